import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HANDLE_W = 22.0          # handle width (X)
HANDLE_D_BOT = 30.6      # handle depth (Y) at the bottom
HANDLE_TAPER = 0.0645    # growth of the +Y face per mm of height
HANDLE_R = 3.0           # handle vertical edge radius
HEAD_W = 32.5            # head width (X)
HEAD_Y1 = 58.0           # head front (+Y) face
SLOPE_Z0 = 86.0          # bottom of the sloped -Y face (at Y=0)
SLOPE_Y1 = 9.5           # top of the sloped face (Y)
SLOPE_Z1 = 103.5         # top of the sloped face (Z)
TOP_Z1 = 107.0           # top at the +Y end
HEAD_BOT_Y1 = 85.2       # head underside height at the +Y end
HEAD_BOT_Z0 = 78.6       # head underside height where it meets the handle
SHOULDER_Y = 23.0        # lowest point of the head/handle shoulder
SHOULDER_Z = 73.5
HEAD_R = 3.5             # head edge radius
HEAD_PROFILE_R = 4.0     # head profile corner radius
SHOULDER_R = 5.0         # shoulder blend radius
DIAG_R = 4.5             # edges of the narrowing sloped face
STRIP_Y = 3.0            # handle continues a little way up the sloped face
JUNCTION_R = 7.0         # concave blend under the head at the +Y face
HANDLE_BOT_R = 1.5       # bottom edge of the handle
THREAD_D = 21.0
THREAD_L = 11.0
THREAD_YC = 19.75
HOLE_D = 11.3            # two holes on the sloped face
HOLE_X = 7.1
HOLE_DEPTH = 3.0         # shallow blind holes
TRIG_D = 11.0            # button hole on the +Y face of the handle
TRIG_Z = 66.3
TRIG_DEPTH = 3.5
POCKET_Y0 = 15.0         # spray-face pocket on top of the head
POCKET_Y1 = 50.4
POCKET_W = 22.0
POCKET_R = 3.0
BORE_D = 17.0            # water passage through the handle
CBORE_D = 16.5           # bore in the thread stub
SLOT_W = 3.4             # slot in the plate between them
CUT_Y = 7.5              # sloped face narrows from head width (top) to handle width (bottom)
POCKET_FLOOR_Z = 90.0    # floor of the spray-face pocket
WELL_W = 18.4            # deeper well above the water passage
WELL_Y1 = 37.5

hw = HANDLE_W / 2.0
Hw = HEAD_W / 2.0


def y_front(z):
    """+Y face of the handle at height z."""
    return HANDLE_D_BOT + HANDLE_TAPER * z


class _Sel(cq.Selector):
    def __init__(self, fn):
        self.fn = fn

    def filter(self, objs):
        return [o for o in objs if self.fn(o)]


# ---------------- helpers ----------------
SL = (SLOPE_Z1 - SLOPE_Z0) / SLOPE_Y1
yj = y_front(HEAD_BOT_Z0)


def rounded_poly(wp, pts, radii):
    """Closed polygon (workplane local coords) with a tangent arc of radius radii[i] at corner i."""
    n = len(pts)
    segs = []
    for i in range(n):
        p, a, c, r = pts[i], pts[i - 1], pts[(i + 1) % n], radii[i]
        if r <= 0:
            segs.append((p, None, p))
            continue
        v1 = (a[0] - p[0], a[1] - p[1])
        l1 = math.hypot(*v1)
        v1 = (v1[0] / l1, v1[1] / l1)
        v2 = (c[0] - p[0], c[1] - p[1])
        l2 = math.hypot(*v2)
        v2 = (v2[0] / l2, v2[1] / l2)
        ang = math.acos(max(-1.0, min(1.0, v1[0] * v2[0] + v1[1] * v2[1])))
        d = r / math.tan(ang / 2.0)
        bis = (v1[0] + v2[0], v1[1] + v2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.sin(ang / 2.0)
        cen = (p[0] + bis[0] * dc, p[1] + bis[1] * dc)
        segs.append(((p[0] + v1[0] * d, p[1] + v1[1] * d),
                     (cen[0] - bis[0] * r, cen[1] - bis[1] * r),
                     (p[0] + v2[0] * d, p[1] + v2[1] * d)))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, mid, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if mid is not None:
            w = w.threePointArc(mid, t2)
    return w.close()


def _pts(e, n=5):
    return [e.positionAt(i / (n - 1.0)) for i in range(n)]


def _on_side(p, tol=1e-3):
    return abs(abs(p.x) - Hw) < tol


def _on_cut(p, tol=1e-3):
    dx, dy = Hw - hw, CUT_Y
    return abs(((abs(p.x) - hw) * dy - p.y * dx) / math.hypot(dx, dy)) < tol


def _on_line(p, a, b, tol=1e-3):
    vy, vz = b[0] - a[0], b[1] - a[1]
    return abs(((p.y - a[0]) * vz - (p.z - a[1]) * vy) / math.hypot(vy, vz)) < tol


def _on_bottom(p, tol=1e-3):
    return (_on_line(p, (0.0, SLOPE_Z0), (SHOULDER_Y, SHOULDER_Z), tol)
            or _on_line(p, (SHOULDER_Y, SHOULDER_Z), (yj, HEAD_BOT_Z0), tol))


def _all(e, f):
    return all(f(p) for p in _pts(e))


EDGE_GROUPS = {
    "outline": lambda e: _all(e, _on_side) and not _all(e, _on_bottom) and not _all(e, _on_cut),
    "diag": lambda e: (_all(e, _on_cut) and not _all(e, _on_side) and not _all(e, _on_bottom)
                       and abs(e.tangentAt(0.5).z) < 0.999 and abs(e.Center().y) > 1e-3),
    "lower": lambda e: ((_all(e, _on_cut) and _all(e, _on_side))
                        or (_all(e, _on_side) and _all(e, _on_bottom))
                        or (_all(e, _on_cut) and _all(e, _on_bottom))),
}


def fillet_group(wp, name, r):
    """Fillet one edge group; fall back to smaller radii (or none) if the kernel refuses."""
    sel = [e for e in wp.edges().vals() if EDGE_GROUPS[name](e)]
    if not sel:
        return wp
    for rr in (r, 0.8 * r, 0.6 * r):
        try:
            out = wp.newObject(sel).fillet(rr)
            if out.val().isValid():
                return out
        except Exception:
            pass
    return wp


# ---------------- head: side profile prism, sloped face narrowing to the handle ----------------
head_pts = [
    (0.0, SLOPE_Z0),
    (SLOPE_Y1, SLOPE_Z1),
    (HEAD_Y1, TOP_Z1),
    (HEAD_Y1, HEAD_BOT_Y1),
    (yj, HEAD_BOT_Z0),
    (SHOULDER_Y, SHOULDER_Z),
]
head_r = [0.0, HEAD_PROFILE_R, HEAD_PROFILE_R, HEAD_PROFILE_R, 0.0, 0.0]
head = rounded_poly(cq.Workplane("YZ", origin=(-Hw, 0, 0)), head_pts, head_r).extrude(HEAD_W)
for sgn in (1, -1):
    dx, dy = Hw - hw, CUT_Y
    wedge = [
        (sgn * (hw - 0.5 * dx), -0.5 * dy),
        (sgn * (Hw + 3.0 * dx), 4.0 * dy),
        (sgn * (Hw + 30.0), 4.0 * dy),
        (sgn * (Hw + 30.0), -20.0),
        (sgn * (hw - 0.5 * dx), -20.0),
    ]
    head = head.cut(cq.Workplane("XY", origin=(0, 0, 50)).polyline(wedge).close().extrude(80))
head = fillet_group(head, "outline", HEAD_R)
head = fillet_group(head, "diag", DIAG_R)
head = fillet_group(head, "lower", SHOULDER_R)

# ---------------- handle: tapered prism ----------------
us = (HEAD_BOT_Y1 - HEAD_BOT_Z0) / (HEAD_Y1 - yj)   # underside slope
handle_pts = [
    (0.0, 0.0),
    (y_front(0.0), 0.0),
    (yj, HEAD_BOT_Z0),
    (yj + 5.0, HEAD_BOT_Z0 + 5.0 * us),
    (yj + 5.0, SLOPE_Z0 + 6.0),
    (STRIP_Y, SLOPE_Z0 + STRIP_Y * SL),
    (0.0, SLOPE_Z0),
]
handle = rounded_poly(cq.Workplane("YZ", origin=(-hw, 0, 0)), handle_pts,
                      [0.0, 0.0, JUNCTION_R, 0.0, 0.0, 0.0, 0.0]).extrude(HANDLE_W)
try:
    handle = handle.edges(_Sel(lambda e: e.geomType() == "LINE" and (
        (abs(e.tangentAt(0.5).z) > 0.95 and e.Center().z < 60)
        or (e.Center().y < STRIP_Y and abs(abs(e.Center().x) - hw) < 1e-3)))).fillet(HANDLE_R)
    handle = handle.faces("<Z").edges().fillet(HANDLE_BOT_R)
except Exception:
    pass

body = handle.union(head)

# ---------------- thread stub (plain rings instead of a helix) ----------------
thread = (
    cq.Workplane("XY", origin=(0, THREAD_YC, -THREAD_L))
    .circle(THREAD_D / 2.0).extrude(THREAD_L)
)
for i in range(4):
    z = -THREAD_L + 1.5 + i * 2.5
    groove = (
        cq.Workplane("XY", origin=(0, THREAD_YC, z))
        .circle(THREAD_D / 2.0 + 1).circle(THREAD_D / 2.0 - 0.8).extrude(1.0)
    )
    thread = thread.cut(groove)
body = body.union(thread)

# ---------------- spray-face pocket on top ----------------
top_slope = (TOP_Z1 - SLOPE_Z1) / (HEAD_Y1 - SLOPE_Y1)
ang = math.atan(top_slope)
pc_y = (POCKET_Y0 + POCKET_Y1) / 2.0
pc_z = SLOPE_Z1 + top_slope * (pc_y - SLOPE_Y1)
top_plane = cq.Plane(origin=(0, pc_y, pc_z), xDir=(1, 0, 0),
                     normal=(0, -math.sin(ang), math.cos(ang)))
plen = POCKET_Y1 - POCKET_Y0
ledge = (
    cq.Workplane(top_plane).workplane(offset=-1.0).sketch()
    .rect(POCKET_W, plen).vertices().fillet(POCKET_R).finalize()
    .extrude(5.0)
)
body = body.cut(ledge)
pocket = (
    cq.Workplane("XY", origin=(0, pc_y, POCKET_FLOOR_Z)).sketch()
    .rect(POCKET_W - 1.6, plen - 1.6).vertices().fillet(POCKET_R - 0.8).finalize()
    .extrude(25.0)
)
body = body.cut(pocket)
# deeper well above the bore, with a steep rear wall
well_prof = [
    (POCKET_Y0 + 0.8, POCKET_FLOOR_Z + 1.0),
    (WELL_Y1, POCKET_FLOOR_Z + 1.0),
    (WELL_Y1, POCKET_FLOOR_Z - 1.0),
    (34.5, POCKET_FLOOR_Z - 3.0),
    (THREAD_YC + BORE_D / 2.0 - 0.5, 70.0),
    (POCKET_Y0 + 0.8, 70.0),
]
well = (
    cq.Workplane("YZ", origin=(-WELL_W / 2.0, 0, 0))
    .polyline(well_prof).close()
    .extrude(WELL_W)
)
body = body.cut(well)
bore = cq.Workplane("XY", origin=(0, THREAD_YC, -6.0)).circle(BORE_D / 2.0).extrude(78.0)
body = body.cut(bore)
cbore = cq.Workplane("XY", origin=(0, THREAD_YC, -THREAD_L - 1)).circle(CBORE_D / 2.0).extrude(4.0)
body = body.cut(cbore)
slot = cq.Workplane("XY", origin=(0, THREAD_YC, -THREAD_L)).rect(BORE_D, SLOT_W).extrude(8.0)
body = body.cut(slot)

# ---------------- two holes on the sloped face ----------------
sy, sz = SLOPE_Y1, SLOPE_Z1 - SLOPE_Z0
L = math.hypot(sy, sz)
n = (0.0, -sz / L, sy / L)  # outward normal of sloped face
t = 0.5
cy, cz = t * SLOPE_Y1, SLOPE_Z0 + t * (SLOPE_Z1 - SLOPE_Z0)
slope_plane = cq.Plane(origin=(0, cy, cz), xDir=(1, 0, 0), normal=n)
holes = (
    cq.Workplane(slope_plane).workplane(offset=1.0)
    .pushPoints([(-HOLE_X, 0), (HOLE_X, 0)]).circle(HOLE_D / 2.0)
    .extrude(-(HOLE_DEPTH + 1.0))
)
body = body.cut(holes)

# ---------------- button hole on the +Y face of the handle ----------------
yf = y_front(TRIG_Z)
trig_plane = cq.Plane(origin=(0, yf, TRIG_Z), xDir=(1, 0, 0),
                      normal=(0, 1, -HANDLE_TAPER))
trig = cq.Workplane(trig_plane).workplane(offset=1.0).circle(TRIG_D / 2.0).extrude(-(TRIG_DEPTH + 1.0))
body = body.cut(trig)

result = body
